import math

import cadquery as cq

# ---------------------------------------------------------------
# Humanoid servo robot with a bear head (units: mm, Z up, face -Y)
# Built from simple features: boxes (servos), U-brackets, spheres,
# discs and a lofted belly.  Right half is built and mirrored.
# ---------------------------------------------------------------

# ---- head ----
HEAD_R = 21.5
HEAD_C = (0.0, -2.5, 206.5)
EAR_R = 10.0
EAR_T = 8.4
EAR_DX = 16.8
EAR_Z = 226.5
MUZZLE_R = 9.5
MUZZLE_C = (0.0, -16.0, 198.5)
EYE_R = 4.8
EYE_DX = 6.9
EYE_Z = 213.8
EYE_Y = -23.3

# ---- neck / torso ----
NECK_W, NECK_Y0, NECK_Y1 = 21.5, -7.5, 6.5
NECK_Z0, NECK_Z1 = 176.0, 188.0
TORSO_W, TORSO_Y0, TORSO_Y1 = 59.0, -15.8, 15.2
TORSO_Z1 = 177.8
TORSO_CHAMFER = 2.0
CHEST_RF = 6.0
CHEST_RB = 9.0
BELLY_W, BELLY_D = 65.0, 41.0
BELLY_Z0, BELLY_Z1 = 128.0, 148.5
PACK_W, PACK_Y0, PACK_Y1 = 42.0, 14.5, 24.0
PACK_Z0, PACK_Z1 = 149.3, 172.3

# ---- arm (+X side, boxes as x0, x1, y0, y1, z0, z1) ----
SHOULDER_BRK = (33.0, 47.5, -13.7, 12.1, 161.5, 175.5)
SHOULDER_SRV = (33.8, 46.7, -9.9, 7.5, 161.5, 174.0)
UPPER_ARM = (33.0, 52.8, -13.5, 12.1, 136.6, 162.5)
ELBOW = (36.0, 51.0, -10.3, 7.4, 118.0, 137.5)
FOREARM = (36.0, 55.6, -12.6, 11.6, 100.4, 119.0)
WRIST = (38.0, 53.0, -13.2, 11.6, 88.0, 101.0)
HAND_X = 48.3

# ---- leg (+X side) ----
PELVIS_LINK = (5.4, 19.6, -9.0, 8.0, 118.0, 129.0)
HIP_BRK = (1.2, 24.2, -9.5, 11.0, 106.9, 120.0)
HIP_SRV = (3.2, 22.0, -8.0, 10.0, 99.0, 116.0)
THIGH = (1.9, 28.5, -7.5, 9.0, 72.3, 99.5)
KNEE_LINK = (6.7, 26.8, -9.0, 8.0, 67.0, 73.5)
SHIN = (5.6, 34.2, -11.5, 8.7, 48.8, 68.0)
SHIN_BRK = (7.8, 33.2, -8.0, 4.5, 35.0, 50.0)
ANKLE_BRK = (16.3, 29.4, -14.4, 9.9, 20.6, 36.2)
ANKLE_SRV = (16.8, 29.0, -11.0, 6.4, 10.0, 34.5)

# ---- foot ----
FOOT_W = 34.6
FOOT_Y0, FOOT_Y1 = -30.0, 20.8
FOOT_T = 10.8
FOOT_XC = 23.3
FOOT_FIL = 3.5

# ---- leg splay (deg, bottoms outward) ----
LEG_SPLAY = 4.5

# ---- bracket plate thickness ----
T_BR = 2.3

VIEW = {"azimuth": 45, "elevation": 26}


def box(x0, x1, y0, y1, z0, z1):
    """Axis aligned box from min/max coordinates."""
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0)
        .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2))
    )


def ubracket(x0, x1, y0, y1, z0, z1, t=T_BR, plates="x", bar="top"):
    """U shaped sheet bracket: two side plates normal to X (or Y)
    joined by a cross bar at the top or bottom."""
    if plates == "x":
        p1 = box(x0, x0 + t, y0, y1, z0, z1)
        p2 = box(x1 - t, x1, y0, y1, z0, z1)
    else:
        p1 = box(x0, x1, y0, y0 + t, z0, z1)
        p2 = box(x0, x1, y1 - t, y1, z0, z1)
    if bar == "top":
        b = box(x0, x1, y0, y1, z1 - t, z1)
    else:
        b = box(x0, x1, y0, y1, z0, z0 + t)
    return p1.union(p2).union(b)


def servo(x0, x1, y0, y1, z0, z1, r=0.8):
    """Servo case: box with lightly broken vertical edges."""
    b = box(x0, x1, y0, y1, z0, z1)
    try:
        return b.edges("|Z").fillet(r)
    except Exception:
        return b


def rolled(shape, cx, cz, ang=None):
    """Roll a leg part outward about a Y-parallel axis through (cx, cz)."""
    a = LEG_SPLAY if ang is None else ang
    return shape.rotate((cx, 0, cz), (cx, 1, cz), -a)


def centre_xz(b):
    """X and Z centre of a (x0, x1, y0, y1, z0, z1) box tuple."""
    return (b[0] + b[1]) / 2.0, (b[4] + b[5]) / 2.0


def cyl_x(x0, x1, y, z, r):
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .center(y, z)
        .circle(r)
        .extrude(x1 - x0)
    )


def hand():
    # gripper: bracket box with an open pocket and a flared round claw
    body = box(HAND_X - 7.8, HAND_X + 7.2, -10.9, 8.8, 78.0, 86.5)
    body = body.cut(box(HAND_X - 5.8, HAND_X + 5.2, -12.0, 6.5, 80.0, 85.0))
    claw = cq.Workplane("XY").add(
        cq.Solid.makeCone(8.5, 6.0, 7.5,
                          pnt=cq.Vector(HAND_X, 0, 71.5),
                          dir=cq.Vector(0, 0, 1)))
    return body.union(claw)


def foot():
    # D-shaped sole: square heel (+Y), round toe (-Y)
    r = FOOT_W / 2.0
    yc = FOOT_Y0 + r
    sk = (
        cq.Workplane("XY")
        .moveTo(-r, FOOT_Y1)
        .lineTo(-r, yc)
        .threePointArc((0, FOOT_Y0), (r, yc))
        .lineTo(r, FOOT_Y1)
        .close()
        .extrude(FOOT_T)
    )
    try:
        sk = sk.faces(">Z").edges().fillet(FOOT_FIL)
    except Exception:
        pass
    return sk.translate((FOOT_XC, 0, 0))


def half_side():
    """Arm and leg parts of the +X side; build() mirrors them to -X."""
    parts = []
    # ---------------- arm ----------------
    parts.append(cyl_x(28.0, SHOULDER_BRK[0] + 1.0, 1.0, 169.0, 3.5))  # shoulder horn
    parts.append(ubracket(*SHOULDER_BRK, plates="y"))             # shoulder bracket
    parts.append(servo(*SHOULDER_SRV))                            # shoulder servo
    parts.append(servo(*UPPER_ARM))                               # upper arm servo
    ex0, ex1, ey0, ey1, ez0, ez1 = ELBOW
    elbow = box(*ELBOW)
    for yy in (ey0, ey1):                                         # framed panels
        elbow = elbow.cut(box(ex0 + 2.5, ex1 - 2.5, yy - 1.6, yy + 1.6,
                              ez0 + 3.0, ez1 - 3.0))
    parts.append(elbow)                                           # elbow bracket
    fx0, fx1, fy0, fy1, fz0, fz1 = FOREARM
    parts.append(servo(*FOREARM))                                 # forearm servo
    for y0, y1 in ((fy0 - 2.3, fy0 + 0.2), (fy1 - 0.2, fy1 + 2.4)):  # side plates
        parts.append(box(fx0 + 1.0, fx1 - 1.0, y0, y1, fz0 + 0.6, fz1 - 0.5))
    wx0, wx1, wy0, wy1, wz0, wz1 = WRIST
    wrist = ubracket(*WRIST, plates="y", bar="top")
    wrist = wrist.union(box(wx0 + 2.0, wx1 - 2.0, wy0 + 3.2, wy1 - 3.1,
                            wz0 - 3.0, wz1 - 2.0))
    parts.append(wrist)                                           # wrist
    parts.append(hand())
    # ---------------- leg ----------------
    parts.append(box(*PELVIS_LINK))                               # pelvis link
    parts.append(ubracket(*HIP_BRK))                              # hip bracket
    parts.append(servo(*HIP_SRV))                                 # hip servo
    # thigh and shin servos are rolled slightly outward (A-stance)
    parts.append(rolled(servo(*THIGH), *centre_xz(THIGH)))        # thigh servo
    parts.append(box(*KNEE_LINK))                                 # knee link
    parts.append(rolled(servo(*SHIN), *centre_xz(SHIN)))          # shin servo
    parts.append(rolled(ubracket(*SHIN_BRK, t=2.5, bar="bottom"),
                        *centre_xz(SHIN_BRK)))                    # shin bracket
    sx0, sx1, sy0, sy1, sz0, sz1 = SHIN_BRK
    tail = (sx0 + 3.2, sx1 - 3.2, sy0 - 2.0, sy1 + 2.0, sz0 + 4.0, sz1 - 1.0)
    parts.append(rolled(box(*tail), *centre_xz(tail)))            # servo tail
    parts.append(ubracket(*ANKLE_BRK, plates="y"))                # ankle bracket
    parts.append(servo(*ANKLE_SRV))                               # ankle servo
    ax0, ax1, ay0, ay1, az0, az1 = ANKLE_SRV
    parts.append(box(ax0 - 1.2, ax1 + 1.2, ay0 - 2.0, ay1 + 2.1,
                     az0, az0 + 8.0))                             # ankle foot mount
    parts.append(foot())
    return parts


def rrect(w, d, rf, rb, z):
    """Rounded rectangle section at height z: front (-Y) corners rf,
    back (+Y) corners rb."""
    sk = (cq.Sketch().rect(w, d)
          .vertices(">Y").fillet(rb).reset()
          .vertices("<Y").fillet(rf))
    return sk.moved(cq.Location(cq.Vector(0, 0, z)))


def belly():
    # pillow shaped belly: loft through rounded rectangles, the top one
    # identical to the chest section so the two blend without a notch
    yc = (TORSO_Y0 + TORSO_Y1) / 2.0
    secs = [
        rrect(BELLY_W - 9.0, BELLY_D - 7.0, 12.0, 12.0, BELLY_Z0),
        rrect(BELLY_W - 1.5, BELLY_D - 1.5, 15.0, 15.0, BELLY_Z0 + 5.0),
        rrect(BELLY_W, BELLY_D, 15.0, 15.0, BELLY_Z0 + 11.0),
        rrect(TORSO_W, TORSO_Y1 - TORSO_Y0, CHEST_RF, CHEST_RB, BELLY_Z1),
    ]
    return (cq.Workplane("XY").placeSketch(*secs).loft()
            .translate((0, yc, 0)))


def ear_shape():
    """Oblate, lens like ear: a four-centre ellipse profile (two tangent
    circular arcs per quadrant) revolved about the Y axis."""
    a, b, r2 = EAR_R, EAR_T / 2.0, EAR_T * 0.3
    big = ((a - r2) ** 2 + b * b - r2 * r2) / (2.0 * (b - r2))
    c1y = b - big
    dx, dy = a - r2, -c1y
    ln = math.hypot(dx, dy)
    px, py = big * dx / ln, c1y + big * dy / ln
    ang_p = math.atan2(dy, dx)
    mid = (math.pi / 2 + ang_p) / 2.0
    mx, my = big * math.cos(mid), c1y + big * math.sin(mid)
    return (
        cq.Workplane("XY")
        .moveTo(0, -b)
        .threePointArc((mx, -my), (px, -py))
        .threePointArc((a, 0), (px, py))
        .threePointArc((mx, my), (0, b))
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )


def head():
    # sphere seam turned to the back so the ears fuse cleanly
    h = (cq.Workplane("XY").sphere(HEAD_R)
         .rotate((0, 0, 0), (0, 0, 1), 90).translate(HEAD_C))
    for s in (-1, 1):
        # ear: lens shaped disc facing the front
        ear = ear_shape().translate((s * EAR_DX, 0, EAR_Z))
        h = h.union(ear)
    # muzzle (sphere poles along Y keep the seams off the head sphere)
    h = h.union(cq.Workplane("XY").sphere(MUZZLE_R)
                .rotate((0, 0, 0), (1, 0, 0), 90).translate(MUZZLE_C))
    # eye sockets
    for s in (-1, 1):
        eye = (cq.Workplane("XY").sphere(EYE_R)
               .rotate((0, 0, 0), (1, 0, 0), 90)
               .translate((s * EYE_DX, EYE_Y, EYE_Z)))
        h = h.cut(eye)
    return h


def torso():
    # chest: extruded rounded rectangle, bevelled along the top
    yc = (TORSO_Y0 + TORSO_Y1) / 2.0
    chest = (
        cq.Workplane("XY")
        .placeSketch(rrect(TORSO_W, TORSO_Y1 - TORSO_Y0,
                           CHEST_RF, CHEST_RB, BELLY_Z1))
        .extrude(TORSO_Z1 - BELLY_Z1)
        .translate((0, yc, 0))
    )
    try:
        chest = chest.faces(">Z").edges().chamfer(TORSO_CHAMFER)
    except Exception:
        pass
    t = chest.union(belly())
    t = t.union(box(-NECK_W / 2, NECK_W / 2, NECK_Y0, NECK_Y1,
                    NECK_Z0, NECK_Z1))
    pack = box(-PACK_W / 2, PACK_W / 2, PACK_Y0, PACK_Y1, PACK_Z0, PACK_Z1)
    try:
        pack = pack.edges("|Y").fillet(1.5)
    except Exception:
        pass
    t = t.union(pack)
    return t


def build():
    body = head().union(torso())
    for p in half_side():
        body = body.union(p).union(p.mirror("YZ"))
    return body


result = build()
